import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions (mm).  Z = 0 is the top face of the mounting plate,
# Y = 0 is the front face of the hanging paddle, X is symmetric.
# ---------------------------------------------------------------------------
PLATE_W = 67.2          # mounting plate width (X)
PLATE_Y0 = -2.1         # plate front edge
PLATE_Y1 = 35.75        # plate rear edge
PLATE_T = 3.7           # plate thickness
SKIRT_D = 8.2           # side skirt depth below top face
SKIRT_W = 1.05          # skirt width at its bottom
ARCH_X = 23.3           # apex of the underside caves
ARCH_R = 11.8           # radius of the cave arc on the skirt side
FRONT_CORNER_R = 1.5    # plan-view radius of the plate front corners
SKIRT_TIP_R = 0.6       # rounding of the skirt's outer bottom edge
SKIRT_FRONT_R = 1.3     # rounding of the skirt's front bottom corner (side view)

TAB_HALF_BASE = 11.8    # tab half-width where it leaves the plate
TAB_APEX_Y = 60.67      # virtual apex of the tapered tab sides
TAB_TOP_R = 9.5         # round top of the tab
TAB_BASE_R = 9.0        # concave blend of the tab into the plate edge
TAB_HOLE_Y = 41.3
TAB_HOLE_D = 5.5

PAD_T = 6.0             # paddle thickness (Y)
NECK_HW = 8.75          # neck half width
NECK_LOW_Z = -39.2      # neck -> shoulder corner
BODY_HW = 26.7          # paddle body half width
SHOULDER_Z = -55.5      # shoulder -> body corner
PAD_BOTTOM = -118.1     # paddle bottom
PAD_CORNER_R = 9.5      # paddle bottom corner radius
NECK_FIL_R = 14.0       # concave neck/shoulder blend
SHOULDER_R = 14.0       # convex shoulder blend
EDGE_R = 2.6            # rounding of the paddle faces
NECK_BLEND_R = 2.0      # blend of the neck front into the plate underside

SLOT_X = 15.3           # slot centre offset
SLOT_W = 3.6
SLOT_Z0 = -54.85
SLOT_Z1 = -112.45

GUSSET_R = 11.15        # rear gusset radius (YZ)
TONGUE_Y0 = 33.0        # rear tongue (lip) front face
TONGUE_Z = -19.9        # rear tongue bottom
TONGUE_CORNER_R = 2.0   # rounding of the tongue's bottom corners
TONGUE_HOLE_Z = -12.0
TONGUE_HOLE_D = 5.0

LUG_HW = 2.55           # lug half thickness (X)
LUG_Z = [-27.6, -99.3]  # lug hole centre heights
LUG_HOLE_Y = -5.25
LUG_HOLE_D = 3.8
LUG_ROOT_R = 1.8        # blend of the lug into the paddle face

FLARE_R = ARCH_X - NECK_HW          # neck flare radius into plate underside
FLARE_Z = -PLATE_T - FLARE_R        # where the flare becomes the neck


# ---------------------------------------------------------------------------
# small 2D helpers
# ---------------------------------------------------------------------------
def _norm(v):
    l = math.hypot(v[0], v[1])
    return (v[0] / l, v[1] / l)


def corner_fillet(p0, p, p1, r):
    """tangent points + arc midpoint of a fillet of radius r at corner p."""
    u1 = _norm((p0[0] - p[0], p0[1] - p[1]))
    u2 = _norm((p1[0] - p[0], p1[1] - p[1]))
    cos_t = max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1]))
    half = math.acos(cos_t) / 2.0
    d = r / math.tan(half)
    t1 = (p[0] + u1[0] * d, p[1] + u1[1] * d)
    t2 = (p[0] + u2[0] * d, p[1] + u2[1] * d)
    b = _norm((u1[0] + u2[0], u1[1] + u2[1]))
    cd = r / math.sin(half)
    c = (p[0] + b[0] * cd, p[1] + b[1] * cd)
    m = (c[0] - b[0] * r, c[1] - b[1] * r)
    return t1, m, t2


def filleted_path(pts, radii):
    """closed polygon with per-vertex fillet radii -> list of segments."""
    n = len(pts)
    segs = []
    corners = []
    for i in range(n):
        r = radii[i]
        if r > 0:
            corners.append(corner_fillet(pts[i - 1], pts[i], pts[(i + 1) % n], r))
        else:
            corners.append((pts[i], None, pts[i]))
    start = corners[0][2]
    cur = start
    for i in range(1, n + 1):
        t1, m, t2 = corners[i % n]
        if math.hypot(t1[0] - cur[0], t1[1] - cur[1]) > 1e-6:
            segs.append(("line", t1))
        if m is not None:
            segs.append(("arc", m, t2))
        cur = t2
    return start, segs


def build_wire(wp, start, segs):
    w = wp.moveTo(*start)
    for s in segs:
        if s[0] == "line":
            w = w.lineTo(*s[1])
        else:
            w = w.threePointArc(s[1], s[2])
    return w.close()


def mirror_segments(start, segs_right):
    """segments of the right half (from start on the axis to end on the
    axis, counter-clockwise) -> closed full profile."""
    pts = [start]
    for s in segs_right:
        pts.append(s[-1])
    full = list(segs_right)
    # walk back down the left side (mirror, reversed)
    rev = []
    for i in range(len(segs_right) - 1, -1, -1):
        s = segs_right[i]
        prev = pts[i]
        tgt = (-prev[0], prev[1])
        if s[0] == "line":
            rev.append(("line", tgt))
        else:
            rev.append(("arc", (-s[1][0], s[1][1]), tgt))
    return start, full + rev


def arc_mid(c, r, a0, a1):
    a = math.radians((a0 + a1) / 2.0)
    return (c[0] + r * math.cos(a), c[1] + r * math.sin(a))


# ---------------------------------------------------------------------------
# XZ cross-section pieces
# ---------------------------------------------------------------------------
HW = PLATE_W / 2.0
ARCH_C = (ARCH_X, -PLATE_T - ARCH_R)
_sk_in = HW - SKIRT_W
_a_end = math.degrees(math.atan2(-SKIRT_D - ARCH_C[1], _sk_in - ARCH_C[0]))
ARCH_MID = arc_mid(ARCH_C, ARCH_R, 90.0, _a_end)
FLARE_C = (ARCH_X, FLARE_Z)
FLARE_MID = arc_mid(FLARE_C, FLARE_R, 90.0, 180.0)


def plate_section():
    """plate + side skirts + underside caves (XZ), right half mirrored."""
    t1, m, t2 = corner_fillet((_sk_in, -SKIRT_D), (HW, -SKIRT_D), (HW, 0.0),
                              SKIRT_TIP_R)
    segs = [
        ("line", (ARCH_X, -PLATE_T)),
        ("arc", ARCH_MID, (_sk_in, -SKIRT_D)),
        ("line", t1),
        ("arc", m, t2),
        ("line", (HW, 0.0)),
        ("line", (0.0, 0.0)),
    ]
    return mirror_segments((0.0, -PLATE_T), segs)


def paddle_section(top_z=-1.0):
    """paddle outline with neck and flares (XZ), right half mirrored."""
    # lower outline as a filleted polyline
    poly = [
        (0.0, PAD_BOTTOM),
        (BODY_HW, PAD_BOTTOM),
        (BODY_HW, SHOULDER_Z),
        (NECK_HW, NECK_LOW_Z),
        (NECK_HW, FLARE_Z),
    ]
    rad = [0, PAD_CORNER_R, SHOULDER_R, NECK_FIL_R, 0]
    segs = []
    cur = poly[0]
    for i in range(1, len(poly)):
        if rad[i] > 0:
            t1, m, t2 = corner_fillet(poly[i - 1], poly[i], poly[i + 1], rad[i])
            segs.append(("line", t1))
            segs.append(("arc", m, t2))
            cur = t2
        else:
            segs.append(("line", poly[i]))
            cur = poly[i]
    # flare into the plate underside
    flare_mid = (FLARE_C[0] - FLARE_R * math.cos(math.radians(45)),
                 FLARE_C[1] + FLARE_R * math.sin(math.radians(45)))
    segs.append(("arc", flare_mid, (ARCH_X, -PLATE_T)))
    segs.append(("line", (ARCH_X, top_z)))
    segs.append(("line", (0.0, top_z)))
    return mirror_segments((0.0, PAD_BOTTOM), segs)


def tongue_section(top_z=-1.0, corner_r=TONGUE_CORNER_R):
    """rear tongue: the material left between the two underside caves
    (circle ARCH_C / ARCH_R on each side), flat bottom, rounded corners."""
    cx, cz = ARCH_C
    # corner blend circle: tangent to the bottom line (from above) and
    # externally tangent to the cave circle
    fz = TONGUE_Z + corner_r
    fx = cx - math.sqrt((ARCH_R + corner_r) ** 2 - (fz - cz) ** 2)
    d = math.hypot(fx - cx, fz - cz)
    t_cave = (cx + ARCH_R * (fx - cx) / d, cz + ARCH_R * (fz - cz) / d)
    t_bot = (fx, TONGUE_Z)
    a0 = math.atan2(t_bot[1] - fz, t_bot[0] - fx)
    a1 = math.atan2(t_cave[1] - fz, t_cave[0] - fx)
    am = (a0 + a1) / 2.0
    m_blend = (fx + corner_r * math.cos(am), fz + corner_r * math.sin(am))
    # cave arc from the blend point up to the apex
    b0 = math.degrees(math.atan2(t_cave[1] - cz, t_cave[0] - cx))
    if b0 < 0:
        b0 += 360.0
    m_cave = arc_mid(ARCH_C, ARCH_R, b0, 90.0)
    segs = [
        ("line", t_bot),
        ("arc", m_blend, t_cave),
        ("arc", m_cave, (ARCH_X, -PLATE_T)),
        ("line", (ARCH_X, top_z)),
        ("line", (0.0, top_z)),
    ]
    return mirror_segments((0.0, TONGUE_Z), segs)


def xz_solid(section, y0, y1):
    """extrude an XZ section from y0 to y1 (y1 > y0)."""
    start, segs = section
    wp = cq.Workplane("XZ", origin=(0, y1, 0))   # normal is -Y
    return build_wire(wp, start, segs).extrude(y1 - y0)


# ---------------------------------------------------------------------------
# mounting plate (plan outline  ∩  cross-section)
# ---------------------------------------------------------------------------
def plate_plan():
    pts = [
        (-HW, PLATE_Y0),
        (HW, PLATE_Y0),
        (HW, PLATE_Y1),
        (TAB_HALF_BASE, PLATE_Y1),
        (0.0, TAB_APEX_Y),
        (-TAB_HALF_BASE, PLATE_Y1),
        (-HW, PLATE_Y1),
    ]
    radii = [FRONT_CORNER_R, FRONT_CORNER_R, 0.4, TAB_BASE_R, TAB_TOP_R,
             TAB_BASE_R, 0.4]
    start, segs = filleted_path(pts, radii)
    wp = cq.Workplane("XY", origin=(0, 0, -SKIRT_D - 1.0))
    return build_wire(wp, start, segs).extrude(SKIRT_D + 1.0)


plate_side = (
    cq.Workplane("YZ", origin=(-HW - 1.0, 0, 0))
    .moveTo(PLATE_Y0, 1.0)
    .lineTo(PLATE_Y0, -SKIRT_D + SKIRT_FRONT_R)
    .radiusArc((PLATE_Y0 + SKIRT_FRONT_R, -SKIRT_D), SKIRT_FRONT_R)
    .lineTo(TAB_APEX_Y, -SKIRT_D)
    .lineTo(TAB_APEX_Y, 1.0)
    .close()
    .extrude(PLATE_W + 2.0)
)
plate = (
    plate_plan()
    .intersect(xz_solid(plate_section(), PLATE_Y0 - 1.0, TAB_APEX_Y))
    .intersect(plate_side)
)
plate = plate.cut(
    cq.Workplane("XY", origin=(0, 0, -PLATE_T - 1))
    .center(0, TAB_HOLE_Y).circle(TAB_HOLE_D / 2.0).extrude(PLATE_T + 2)
)

# ---------------------------------------------------------------------------
# paddle with neck and rear gusset (one body), rounded edges, slots
#   XZ outline (neck flaring into the plate underside)
#   ∩ YZ thickness profile (quarter-round gusset behind the neck)
# ---------------------------------------------------------------------------
g_c = (PAD_T + GUSSET_R, FLARE_Z - 1.05)
g_top = (g_c[0], g_c[1] + GUSSET_R)
g_mid = (g_c[0] - GUSSET_R * math.cos(math.radians(45)),
         g_c[1] + GUSSET_R * math.sin(math.radians(45)))
g_far = g_top[0] + (-PLATE_T - g_top[1])

thick_yz = (
    cq.Workplane("YZ", origin=(-HW - 1.0, 0, 0))
    .moveTo(0.0, -1.0)
    .lineTo(g_far, -1.0)
    .lineTo(g_far, -PLATE_T)
    .lineTo(*g_top)
    .threePointArc(g_mid, (PAD_T, g_c[1]))
    .lineTo(PAD_T, PAD_BOTTOM - 1.0)
    .lineTo(0.0, PAD_BOTTOM - 1.0)
    .close()
    .extrude(PLATE_W + 2.0)
)
paddle = xz_solid(paddle_section(), 0.0, g_far + 1.0).intersect(thick_yz)


class _RoundEdges(cq.Selector):
    """outline edges of the paddle body below the plate (skip the straight
    extrusion seams running along Y and the tangent seams along X)."""

    def __init__(self, z):
        self.z = z

    def filter(self, objs):
        out = []
        for e in objs:
            c = e.Center()
            if c.z >= self.z:
                continue
            if e.geomType() == "LINE":
                t = e.tangentAt(0.5)
                if abs(t.y) > 0.99:
                    continue
                if abs(t.x) > 0.99 and c.z > PAD_BOTTOM + 1.0:
                    continue
            out.append(e)
        return out


paddle = paddle.edges(_RoundEdges(-PLATE_T - 0.3)).fillet(EDGE_R)

slot_len = SLOT_Z0 - SLOT_Z1
slots = (
    cq.Workplane("XZ", origin=(0, PAD_T + 1, 0))
    .pushPoints([(-SLOT_X, (SLOT_Z0 + SLOT_Z1) / 2), (SLOT_X, (SLOT_Z0 + SLOT_Z1) / 2)])
    .slot2D(slot_len, SLOT_W, angle=90)
    .extrude(PAD_T + 2)
)
paddle = paddle.cut(slots)

# ---------------------------------------------------------------------------
# rear tongue with hole
# ---------------------------------------------------------------------------
tongue = xz_solid(tongue_section(), TONGUE_Y0, PLATE_Y1)
tongue = tongue.cut(
    cq.Workplane("XZ", origin=(0, PLATE_Y1 + 1, 0))
    .center(0, TONGUE_HOLE_Z).circle(TONGUE_HOLE_D / 2.0)
    .extrude(PLATE_Y1 - TONGUE_Y0 + 2)
)

# ---------------------------------------------------------------------------
# cable lugs on the paddle front
# ---------------------------------------------------------------------------
LUG_PTS = [(0.0, 15.0), (-1.4, 12.2), (-3.6, 9.8), (-6.2, 7.6), (-8.3, 4.6),
           (-9.1, 0.0), (-8.3, -4.6), (-6.0, -7.6), (-3.3, -9.6),
           (-1.3, -11.6), (0.0, -14.2)]


def lug(zc):
    pts = [(y, z + zc) for (y, z) in LUG_PTS]
    body = (
        cq.Workplane("YZ", origin=(-LUG_HW, 0, 0))
        .moveTo(1.0, pts[0][1])
        .lineTo(*pts[0])
        .spline(pts[1:], includeCurrent=True)
        .lineTo(1.0, pts[-1][1])
        .close()
        .extrude(2 * LUG_HW)
    )
    hole = (
        cq.Workplane("YZ", origin=(-LUG_HW - 1, 0, 0))
        .center(LUG_HOLE_Y, zc).circle(LUG_HOLE_D / 2.0)
        .extrude(2 * LUG_HW + 2)
    )
    return body.cut(hole)


class _LugBase(cq.Selector):
    """root edges of a lug on the paddle front face."""

    def __init__(self, zc):
        self.zc = zc

    def filter(self, objs):
        out = []
        for e in objs:
            bb = e.BoundingBox()
            if (bb.ymin > -0.01 and bb.ymax < 0.01
                    and bb.xmin > -LUG_HW - 0.01 and bb.xmax < LUG_HW + 0.01
                    and bb.zmin > self.zc - 16 and bb.zmax < self.zc + 16):
                out.append(e)
        return out


def lug_with_root(zc):
    """lug on a thin pad that sits inside the paddle, root edges blended."""
    half_len = 15.0 + LUG_ROOT_R + 0.6
    pad = (
        cq.Workplane("XY", origin=(0, 0, zc - half_len))
        .center(0, 0.5)
        .rect(2 * (LUG_HW + LUG_ROOT_R + 0.6), 1.0)
        .extrude(2 * half_len)
    )
    body = pad.union(lug(zc))
    return body.edges(_LugBase(zc)).fillet(LUG_ROOT_R)


for zc in LUG_Z:
    paddle = paddle.union(lug_with_root(zc))

result = plate.union(paddle).union(tongue)


class _NeckFrontRoot(cq.Selector):
    """concave edge where the flat neck front meets the plate underside."""

    def filter(self, objs):
        out = []
        for e in objs:
            bb = e.BoundingBox()
            if (abs(bb.ymin) < 0.05 and abs(bb.ymax) < 0.05
                    and bb.zmin > -PLATE_T - 0.3 and bb.zmax < -PLATE_T + 0.3):
                out.append(e)
        return out


result = result.edges(_NeckFrontRoot()).fillet(NECK_BLEND_R)

VIEW = {"azimuth": 45, "elevation": 26}
